import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 18.2            # thickness along X
LOBE_Y = 20.8       # hex lobe centre offset along Y
LOBE_Z = 10.15      # hex lobe centre height
HEX_AF_IN = 12.65   # nut pocket across flats
HEX_AF_OUT = 17.6   # outer lobe across flats
Z_BOT = 5.08        # flat underside between the lobes
Z_TOP = 39.2        # main top
Z_TAB = 40.6        # front lip top
Z_STEP = 32.6       # rear low step
Z_NOTCH = 36.55     # floor of the cross notch on top
Y_BACK = 27.5       # rear face of the body
Y_FRONT = -27.5     # front face of the body (vertical part)
Y_LIP = -29.75      # front lip overhang

HX = W / 2.0
R_OUT = HEX_AF_OUT / 2.0 / math.cos(math.radians(30))
R_IN = HEX_AF_IN / 2.0 / math.cos(math.radians(30))
YO = LOBE_Y + HEX_AF_OUT / 2.0      # outer flat of lobes (29.6)

# ---------------- side profile (Y,Z) extruded through X ----------------
Z_LV = LOBE_Z - R_OUT / 2          # lower side vertex of lobes (= Z_BOT)
Z_UV = LOBE_Z + R_OUT / 2          # upper side vertex of lobes
# moulded rear face: lobe flat -> shoulder -> vertical rear face (one smooth face)
rear_pts = [(YO, 10.0), (YO, 13.6), (Y_BACK + 1.75, 15.9), (Y_BACK + 0.8, 18.3),
            (Y_BACK + 0.15, 20.5), (Y_BACK, 24.0), (Y_BACK, Z_STEP)]
# moulded front face: overhanging lip -> vertical -> shoulder (one smooth face)
front_pts = [(Y_FRONT - 1.15, 35.2), (Y_FRONT - 0.25, 30.5), (Y_FRONT, 28.2),
             (Y_FRONT, 25.0), (Y_FRONT + 0.4, 22.6), (Y_FRONT + 1.0, 20.2)]
body = (cq.Workplane("YZ").workplane(offset=-HX)
        .moveTo(-LOBE_Y, LOBE_Z - R_OUT)
        .lineTo(-LOBE_Y + HEX_AF_OUT / 2, Z_BOT)
        .lineTo(LOBE_Y - HEX_AF_OUT / 2, Z_BOT)
        .lineTo(LOBE_Y, LOBE_Z - R_OUT)
        .lineTo(YO, Z_LV)
        .spline(rear_pts, tangents=[(0, 1), (0, 1)], includeCurrent=True, scale=False)
        .lineTo(16.4, Z_STEP)                    # rear low step
        .lineTo(16.4, 35.35)
        .lineTo(17.1, 35.35)                     # small overhang of the top plate
        .lineTo(17.1, Z_TOP)
        .lineTo(-25.95, Z_TOP)
        .lineTo(-25.95, Z_TAB)                   # front lip
        .lineTo(Y_LIP, Z_TAB)
        .spline(front_pts, tangents=[(0.2, -1), (0.22, -0.98)], includeCurrent=True,
                scale=False)
        .lineTo(-YO, Z_UV)                       # shoulder into the front lobe
        .lineTo(-YO, Z_LV)
        .close()
        .extrude(W))


def fillet_x_edges(wp, spots, r):
    """fillet the X-parallel profile edges located at the given (Y, Z) spots"""
    def near(e):
        c = e.Center()
        return any(abs(c.y - y) < 0.05 and abs(c.z - z) < 0.05 for (y, z) in spots)
    edges = [e for e in wp.edges("|X").vals() if near(e)]
    solid = wp.val().fillet(r, edges)
    return cq.Workplane("XY").add(solid)


# rounded lip on the front and rounded rear shoulder
body = fillet_x_edges(body, [(Y_BACK, Z_STEP)], 0.8)
body = fillet_x_edges(body, [(Y_LIP, Z_TAB)], 0.9)
body = fillet_x_edges(body, [(-25.95, Z_TAB)], 0.6)
# small round on the outline of both side faces
R_SIDE = 0.7
try:
    body = body.faces(">X or <X").edges().fillet(R_SIDE)
except Exception:
    body = body.faces(">X or <X").edges().fillet(0.5)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(y, z, r, x0, x1):
    return (cq.Workplane("YZ").workplane(offset=x0)
            .center(y, z).circle(r).extrude(x1 - x0))


def cyl_y(x, z, r, y0, y1):
    return (cq.Workplane("XZ").workplane(offset=-y0)
            .center(x, z).circle(r).extrude(-(y1 - y0)))


def cyl_z(x, y, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(r).extrude(z1 - z0))


# ---------------- hex nut pockets through X ----------------
R_HEX_RIM = 0.8
for sgn in (-1, 1):
    hexcut = (cq.Workplane("YZ").workplane(offset=-HX - 1)
              .center(sgn * LOBE_Y, LOBE_Z)
              .transformed(rotate=(0, 0, 90))      # vertices up / down
              .polygon(6, 2 * R_IN).extrude(W + 2))
    body = body.cut(hexcut)


def _on_hex_rim(e):
    c = e.Center()
    return (abs(abs(c.x) - HX) < 0.05 and
            math.hypot(abs(c.y) - LOBE_Y, c.z - LOBE_Z) < R_IN + 0.05)


rim = [e for e in body.edges().vals() if _on_hex_rim(e)]
try:
    body = cq.Workplane("XY").add(body.val().fillet(R_HEX_RIM, rim))
except Exception:
    pass

# ---------------- central slot through X ----------------
SLOT_Y0, SLOT_Y1, SLOT_Z = 0.7, 7.6, 19.4
body = body.cut(box(-HX - 1, HX + 1, SLOT_Y0, SLOT_Y1, -1, SLOT_Z))

# ---------------- key-hole slit on the underside ----------------
SLIT_Y0, SLIT_Y1, SLIT_Z = -6.85, -4.35, 12.65
body = body.cut(box(0.0, HX + 1, SLIT_Y0, SLIT_Y1, -1, SLIT_Z))
body = body.cut(cyl_z(0.0, (SLIT_Y0 + SLIT_Y1) / 2, 2.2, -1, SLIT_Z))

# rounded vertical mouth edges of slot and slit on the side faces
R_MOUTH = 0.6


def _mouth_edge(e):
    c = e.Center()
    if abs(abs(c.x) - HX) > 0.05 or not (Z_BOT + 0.6 < c.z < SLOT_Z):
        return False
    ys = (SLOT_Y0, SLOT_Y1) + ((SLIT_Y0, SLIT_Y1) if c.x > 0 else ())
    return any(abs(c.y - y) < 0.05 for y in ys)


mouth = [e for e in body.edges("|Z").vals() if _mouth_edge(e)]
try:
    body = cq.Workplane("XY").add(body.val().fillet(R_MOUTH, mouth))
except Exception:
    pass

# ---------------- side holes through X (counterbored on +X) ----------------
CB_DEPTH = 3.0
for (hy, hz) in ((15.6, 25.1), (-18.35, 22.5)):
    body = body.cut(cyl_x(hy, hz, 1.33, -HX - 1, HX + 1))
    body = body.cut(cyl_x(hy, hz, 2.62, HX - CB_DEPTH, HX + 1))

# ---------------- cross notch on top (joins the channel on -X side) ----------------
NOTCH_Y0, NOTCH_Y1 = -0.65, 2.8
CH_WALL_X = -4.6          # -X wall of the rear block below the notch
R_NC = 1.4                # rounded corner between notch floor and that wall
notch = (cq.Workplane("XZ").workplane(offset=-NOTCH_Y1)
         .moveTo(-HX - 1, 25.7).lineTo(CH_WALL_X, 25.7)
         .lineTo(CH_WALL_X, Z_NOTCH - R_NC)
         .threePointArc((CH_WALL_X + R_NC - R_NC * math.cos(math.radians(45)),
                         Z_NOTCH - R_NC + R_NC * math.sin(math.radians(45))),
                        (CH_WALL_X + R_NC, Z_NOTCH))
         .lineTo(HX + 1, Z_NOTCH).lineTo(HX + 1, Z_TAB + 1)
         .lineTo(-HX - 1, Z_TAB + 1).close()
         .extrude(NOTCH_Y1 - NOTCH_Y0))
body = body.cut(notch)

# ---------------- rear top plate with L-shaped outline ----------------
L_X = -0.7                # X of the step in the outline
R_LO, R_LI = 1.2, 0.8      # outer / inner corner rounds of the L outline


def l_cutter(y_in, y_out, z0, z1):
    """remove X < L_X beyond y_in, and round the outer corner at (L_X, y_out)"""
    c45 = math.cos(math.radians(45))
    return (cq.Workplane("XY").workplane(offset=z0)
            .moveTo(-HX - 1, y_in)
            .lineTo(L_X - R_LI, y_in)
            .threePointArc((L_X - R_LI + R_LI * c45, y_in + R_LI - R_LI * c45),
                           (L_X, y_in + R_LI))
            .lineTo(L_X, y_out - R_LO)
            .threePointArc((L_X + R_LO - R_LO * c45, y_out - R_LO + R_LO * c45),
                           (L_X + R_LO, y_out))
            .lineTo(L_X + R_LO, y_out + 1)
            .lineTo(-HX - 1, y_out + 1)
            .close()
            .extrude(z1 - z0))


body = body.cut(l_cutter(12.7, 17.1, 35.35, Z_TAB + 1))
body = body.cut(l_cutter(12.0, 16.4, Z_STEP, 35.35))

# cove under the overhang of the rear plate (rounded into the low step)
R_COVE = 1.0


def _cove_edge(e):
    bb = e.BoundingBox()
    c = e.Center()
    return (abs(bb.zmin - Z_STEP) < 1e-3 and abs(bb.zmax - Z_STEP) < 1e-3
            and 11.5 < c.y < 17.0 and abs(c.x) < HX - 0.5)


try:
    body = cq.Workplane("XY").add(
        body.val().fillet(R_COVE, [e for e in body.edges().vals() if _cove_edge(e)]))
except Exception:
    pass

# ---------------- front lip only on +X part ----------------
body = body.cut(box(-HX - 1, -1.4, -31, -25.95, Z_TOP, Z_TAB + 1))

# ---------------- wire channel on -X side of the front part ----------------
CH_X, CH_Z, CH_R = -3.0, 33.4, 5.3       # concave channel wall (C profile)
PLATE_EDGE = -3.45                        # -X edge of the top plate
FLOOR_Z = 25.7                            # channel floor
BACK_FACE_Y = -0.65                       # channel end (rear block face)
PLATE_CUT_Z = 35.5                        # below this the channel profile rules
R_FLOOR = 1.25                            # round between channel floor and wall
c45 = math.cos(math.radians(45))
ch_low = (cq.Workplane("XZ").workplane(offset=-BACK_FACE_Y)
          .moveTo(-HX - 1, FLOOR_Z)
          .lineTo(PLATE_EDGE - R_FLOOR, FLOOR_Z)
          .threePointArc((PLATE_EDGE - R_FLOOR + R_FLOOR * c45,
                          FLOOR_Z + R_FLOOR - R_FLOOR * c45),
                         (PLATE_EDGE, FLOOR_Z + R_FLOOR))
          .lineTo(PLATE_EDGE, PLATE_CUT_Z + 0.01)
          .lineTo(-HX - 1, PLATE_CUT_Z + 0.01)
          .close()
          .extrude(31 + BACK_FACE_Y))
body = body.cut(ch_low)
body = body.cut(cyl_y(CH_X, CH_Z, CH_R, -31, BACK_FACE_Y))
# -X edge of the top plate: S-shaped tongue/bite near the rear block,
# straight further forward, rounded into the front lip
plate_edge = (cq.Workplane("XY").workplane(offset=PLATE_CUT_Z)
              .moveTo(-HX - 1, BACK_FACE_Y)
              .lineTo(-1.5, BACK_FACE_Y)
              .spline([(-2.8, -2.66), (-1.84, -5.24), (1.31, -7.22), (1.74, -8.4),
                       (0.45, -10.67), (-2.4, -12.5), (-3.4, -15.5)],
                      tangents=[(-1.0, -1.4), (0.0, -1.5)], includeCurrent=True,
                      scale=False)
              .lineTo(-3.4, -24.5)
              .spline([(-2.7, -26.6), (-1.5, -27.6)],
                      tangents=[(0.0, -1.0), (0.3, -1.0)], includeCurrent=True,
                      scale=False)
              .lineTo(-1.5, -31).lineTo(-HX - 1, -31).close()
              .extrude(Z_TAB + 1 - PLATE_CUT_Z))
body = body.cut(plate_edge)
# wire entry hole in the rear block face (with small counterbore)
body = body.cut(cyl_y(-1.5, 33.6, 1.4, BACK_FACE_Y - 0.5, 8.0))
body = body.cut(cyl_y(-1.5, 33.6, 2.1, BACK_FACE_Y - 0.5, BACK_FACE_Y + 0.6))
# set-back, rounded front of the block below the channel
lb = (cq.Workplane("XY").workplane(offset=20.2)
      .moveTo(-HX - 1, -24.8).lineTo(-2.3, -24.8)
      .radiusArc((-1.5, -25.6), 0.8)
      .lineTo(-1.5, -31).lineTo(-HX - 1, -31).close()
      .extrude(28.0 - 20.2))
body = body.cut(lb)

# ---------------- vertical holes ----------------
H1_X, H1_Y = 4.15, 20.85                      # through hole over the rear nut pocket
body = body.cut(cyl_z(H1_X, H1_Y, 1.4, LOBE_Z, Z_STEP + 1))
body = body.cut(cyl_z(H1_X, H1_Y, 2.3, -1, 19.0))  # larger bore through the pocket
body = body.cut(cyl_z(3.7, 13.9, 1.2, Z_TOP - 10, Z_TOP + 1))  # blind
body = body.cut(cyl_z(4.3, -21.8, 1.8, Z_TOP - 12.0, Z_TOP + 2))

# ---------------- small windows on the -X face ----------------
body = body.cut(box(-HX - 1, -HX + 3, 19.8, 22.0, 19.6, 27.2))
body = body.cut(box(-HX - 1, -HX + 3, -7.27, -1.73, 22.2, 23.95))

result = body
